import math
import cadquery as cq

# ---------------- Frame (120 mm fan housing) ----------------
W = 120.0          # square frame size
H = 23.5           # frame height
TF = 2.5           # flange thickness
RC = 2.0           # corner radius of flanges
R_BORE = 56.0      # venturi bore radius
R_OUT = 59.8       # venturi outer radius
CH_R = 5.8         # chamfer between venturi and flanges: radial size
CH_Z = 5.0         # chamfer vertical size
HOLE_D = 5.6       # mounting hole diameter
HOLE_OFF = 55.0    # mounting hole offset from centre
FLARE_R = 64.0     # inlet/outlet flare radius at the faces
FLARE_D = 4.0      # flare depth
FLARE_IN = 59.4    # flare is kept inside this half-width at the faces (thin rim)
FLARE_WALL = 0.62  # inward slope (mm per mm of depth) of the rim wall
BLK_S_X0 = -21.0   # -Y face solid block, x range
BLK_S_X1 = 19.8
BLK_N_C0 = 25.8    # +Y face solid block bounded by x+y >= C0 ...
BLK_N_C1 = 98.6    # ... and x+y <= C1
RIB_T = 1.2        # corner rib thickness
RIB_R0 = 52.0      # corner rib start radius
RIB_R1 = 73.5      # corner rib end radius

HUB_R = 25.0       # motor mount disc radius
HUB_HOLE_D = 12.0  # centre hole
HUB_T = 3.0        # disc / spoke height
HUB_RECESS = 1.0   # shallow conical recess on the underside of the disc
SPOKE_W = 3.8      # thin spoke width
WIDE_A0 = 15.9     # wide spoke: distance of lower edge from centre
WIDE_A1 = 24.7     # wide spoke: distance of upper edge from centre (tangent to hub)
WIDE_N = (0.374, 0.927)
CH_W = 5.0         # wire channel width under the wide spoke
CH_D = 1.6         # wire channel depth

# ---------------- Impeller ----------------
IMP_X = 140.0
IMP_Y = -56.5
IMP_R_TIP = 55.5
IMP_R_HUB = 22.5
IMP_H = 15.5
IMP_CUP_H = 15.8
IMP_WALL = 1.2
N_BLADES = 8
BLADE_T = 1.0
BLADE_PHASE = 25.5     # angle of the blade root edge (bottom) of blade 0
SWEEP_HUB = 46.7       # angular travel of the blade over its height at the hub
SWEEP_TIP = 38.2       # angular travel at the tip
BLADE_CAMBER = 0.66    # fraction of the angular travel reached at mid-height


def square_plate(z0, t, half=W / 2, rc=RC):
    return (cq.Workplane("XY").workplane(offset=z0)
            .rect(2 * half, 2 * half).extrude(t)
            .edges("|Z").fillet(rc))


def revolve_profile(pts):
    """Revolve a closed polyline given in (r, z) around the Z axis."""
    return cq.Workplane("XZ").polyline(pts).close().revolve(360, (0, 0, 0), (0, 1, 0))


# flanges
frame = square_plate(0, TF).union(square_plate(H - TF, TF))

# venturi tube (outer)
SEAM = 45.0        # angular position of cylinder / cone seams (kept on silhouettes)
tube = cq.Workplane("XY").circle(R_OUT).extrude(H).rotate((0, 0, 0), (0, 0, 1), SEAM)
frame = frame.union(tube)

# chamfer rings between tube and flanges
_s = CH_Z / CH_R
ring_bot = revolve_profile([(R_OUT - 1.0, TF - 0.01), (R_OUT + CH_R, TF - 0.01),
                            (R_OUT - 1.0, TF + CH_Z + _s)])
ring_top = revolve_profile([(R_OUT - 1.0, H - TF + 0.01), (R_OUT + CH_R, H - TF + 0.01),
                            (R_OUT - 1.0, H - TF - CH_Z - _s)])
frame = (frame.union(ring_bot.rotate((0, 0, 0), (0, 0, 1), SEAM))
         .union(ring_top.rotate((0, 0, 0), (0, 0, 1), SEAM)))

# solid side block on the -Y face (square ends)
blk = (cq.Workplane("XY")
       .polyline([(BLK_S_X0, -W / 2), (BLK_S_X1, -W / 2), (BLK_S_X1, -40.0), (BLK_S_X0, -40.0)])
       .close().extrude(H))
frame = frame.union(blk)
# wider solid block on the +Y face, its ends bevelled parallel to the diagonal
blk = (cq.Workplane("XY")
       .polyline([(BLK_N_C0 - W / 2, W / 2), (BLK_N_C1 - W / 2, W / 2),
                  (BLK_N_C1 / 2, BLK_N_C1 / 2), (30.0, 30.0),
                  (BLK_N_C0 - 35.0, 35.0)])
       .close().extrude(H))
frame = frame.union(blk)

# thin diagonal corner ribs
for ang in (45, 135, 225, 315):
    rib = (cq.Workplane("XY").center((RIB_R0 + RIB_R1) / 2, 0)
           .rect(RIB_R1 - RIB_R0, RIB_T).extrude(H)
           .rotate((0, 0, 0), (0, 0, 1), ang))
    frame = frame.union(rib)

# trim everything to the square outline
frame = frame.intersect(square_plate(0, H))

# bore
bore = (cq.Workplane("XY").workplane(offset=-1).circle(R_BORE).extrude(H + 2)
        .rotate((0, 0, 0), (0, 0, 1), SEAM))
frame = frame.cut(bore)

# conical inlet / outlet flares, kept inside a thin outer rim
_k = (FLARE_R - R_BORE) / FLARE_D
_ext = 3.0
flare_top = cq.Solid.makeCone(R_BORE, R_BORE + _k * (FLARE_D + _ext), FLARE_D + _ext,
                              cq.Vector(0, 0, H - FLARE_D))
flare_bot = cq.Solid.makeCone(R_BORE + _k * (FLARE_D + _ext), R_BORE, FLARE_D + _ext,
                              cq.Vector(0, 0, -_ext))


def rim_clip(z_face, direction):
    """Square frustum: FLARE_IN half-width at the face, narrowing inward."""
    a_out = FLARE_IN + 1.0 * FLARE_WALL
    a_in = FLARE_IN - (FLARE_D + 2.0) * FLARE_WALL
    z_out = z_face + direction * 1.0
    z_in = z_face - direction * (FLARE_D + 2.0)
    w_out = cq.Wire.makePolygon([cq.Vector(sx * a_out, sy * a_out, z_out)
                                 for sx, sy in ((1, 1), (-1, 1), (-1, -1), (1, -1))], close=True)
    w_in = cq.Wire.makePolygon([cq.Vector(sx * a_in, sy * a_in, z_in)
                                for sx, sy in ((1, 1), (-1, 1), (-1, -1), (1, -1))], close=True)
    return cq.Solid.makeLoft([w_out, w_in], True)


rim_box = cq.Workplane("XY").add(rim_clip(H, 1)).union(cq.Workplane("XY").add(rim_clip(0, -1)))
flares = flare_top.fuse(flare_bot).intersect(rim_box.val())
frame = frame.cut(cq.Workplane("XY").add(flares))

# mounting holes
holes = (cq.Workplane("XY").workplane(offset=-1)
         .rect(2 * HOLE_OFF, 2 * HOLE_OFF, forConstruction=True).vertices()
         .circle(HOLE_D / 2).extrude(H + 2))
frame = frame.cut(holes)

# ---- motor mount: hub disc + spokes ----
R_SPOKE_END = R_OUT - 0.5


def bar(p0, p1, w, h):
    dx, dy = p1[0] - p0[0], p1[1] - p0[1]
    L = math.hypot(dx, dy)
    ang = math.degrees(math.atan2(dy, dx))
    cx, cy = (p0[0] + p1[0]) / 2, (p0[1] + p1[1]) / 2
    return (cq.Workplane("XY").rect(L, w).extrude(h)
            .rotate((0, 0, 0), (0, 0, 1), ang).translate((cx, cy, 0)))


def extend(p0, p1, r_end):
    """Point on the ray p0->p1 that lies on radius r_end."""
    dx, dy = p1[0] - p0[0], p1[1] - p0[1]
    L = math.hypot(dx, dy)
    ux, uy = dx / L, dy / L
    b = p0[0] * ux + p0[1] * uy
    c = p0[0] ** 2 + p0[1] ** 2 - r_end ** 2
    t = -b + math.sqrt(b * b - c)
    return (p0[0] + t * ux, p0[1] + t * uy)


mount = cq.Workplane("XY").circle(HUB_R).extrude(HUB_T)

thin_spokes = [((24.7, 8.4), (46.95, 28.7)),
               ((13.2, -22.2), (34.45, -44.0)),
               ((-20.9, -15.0), (-39.05, -39.7))]
for p0, p1 in thin_spokes:
    dx, dy = p1[0] - p0[0], p1[1] - p0[1]
    L = math.hypot(dx, dy)
    q0 = (p0[0] - 6 * dx / L, p0[1] - 6 * dy / L)
    q1 = extend(p0, p1, R_SPOKE_END + 2)
    mount = mount.union(bar(q0, q1, SPOKE_W, HUB_T))

# wide spoke (wire channel)
nx, ny = WIDE_N
dxw, dyw = -ny, nx   # outward direction
amid = (WIDE_A0 + WIDE_A1) / 2
w_wide = WIDE_A1 - WIDE_A0
p0 = (amid * nx, amid * ny)
p1 = extend(p0, (p0[0] + dxw, p0[1] + dyw), R_SPOKE_END + 2)
wide = bar(p0, p1, w_wide, HUB_T)
q0 = (p0[0] + 6.0 * dxw, p0[1] + 6.0 * dyw)
q1 = extend(p0, (p0[0] + dxw, p0[1] + dyw), 95.0)
channel = bar(q0, q1, CH_W, CH_D).translate((0, 0, -0.01))
mount = mount.union(wide)

# clip spokes inside the venturi wall
mount = mount.intersect(cq.Workplane("XY").circle(R_SPOKE_END).extrude(HUB_T))
mount = mount.cut(cq.Workplane("XY").workplane(offset=-1).circle(HUB_HOLE_D / 2).extrude(HUB_T + 2))
recess = cq.Solid.makeCone(HUB_R - 1.5, HUB_HOLE_D / 2, HUB_RECESS, cq.Vector(0, 0, 0))
mount = mount.cut(cq.Workplane("XY").add(recess))

frame = frame.union(mount).cut(channel)

# ---------------- Impeller ----------------
cup = (cq.Workplane("XY").circle(IMP_R_HUB).extrude(IMP_CUP_H)
       .faces(">Z").workplane().circle(IMP_R_HUB - IMP_WALL).cutBlind(-(IMP_CUP_H - IMP_WALL))
       .rotate((0, 0, 0), (0, 0, 1), 45))   # seam on the silhouette
imp = cup
r_in = IMP_R_HUB - IMP_WALL / 2


def blade_section(z, frac, theta):
    """Thin straight section of a blade at height z (frac = z / height)."""
    ah = math.radians(theta + SWEEP_HUB * frac)
    at = math.radians(theta + SWEEP_TIP * frac)
    ph = (r_in * math.cos(ah), r_in * math.sin(ah))
    pt = (IMP_R_TIP * math.cos(at), IMP_R_TIP * math.sin(at))
    dx, dy = pt[0] - ph[0], pt[1] - ph[1]
    L = math.hypot(dx, dy)
    nx_, ny_ = -dy / L * BLADE_T / 2, dx / L * BLADE_T / 2
    pts = [(ph[0] - nx_, ph[1] - ny_, z), (pt[0] - nx_, pt[1] - ny_, z),
           (pt[0] + nx_, pt[1] + ny_, z), (ph[0] + nx_, ph[1] + ny_, z)]
    return cq.Wire.makePolygon([cq.Vector(*p) for p in pts], close=True)


def make_blade(theta):
    # three sections: root (z=0), mid-height (cambered: more of the turn in the
    # lower half) and top
    secs = [blade_section(IMP_H * t, f, theta)
            for t, f in ((0.0, 0.0), (0.5, BLADE_CAMBER), (1.0, 1.0))]
    return cq.Solid.makeLoft(secs, False)


for i in range(N_BLADES):
    imp = imp.union(cq.Workplane("XY").add(make_blade(BLADE_PHASE + i * 360.0 / N_BLADES)))
imp = imp.translate((IMP_X, IMP_Y, 0))

result = frame.union(imp)
